import cadquery as cq

# ---------------------------------------------------------------------------
# Stacked two-board electronics module (carrier PCB with pin headers, mini-USB
# receptacle and SMD parts, plus a smaller daughter PCB underneath joined by
# stacking pins / female sockets).
# Coordinates: top-board centre at X=Y=0, top-board upper surface at Z=0.
# ---------------------------------------------------------------------------

PITCH = 2.54

# top board
TB_W = 30.48          # along X
TB_L = 49.53          # along Y
TB_T = 1.6

# lower (daughter) board
GAP = 3.0             # clear gap between the two boards
LB_T = 1.2
LB_X0, LB_X1 = -14.5, 11.4
LB_Y0, LB_Y1 = -19.0, 14.65
LB_TOP = -TB_T - GAP
LB_BOT = LB_TOP - LB_T

# pins
PIN_W = 0.64
HDR_BASE_H = 2.5      # plastic body of the pin headers
HDR_PIN_TOP = 8.5     # pin tip height above top board
HDR_PIN_BELOW = 1.25  # pin stub under the top board
STK_PIN_TOP = 4.9     # stacking pin tip height above the top board
STK_PIN_BELOW = 2.0   # stacking pin length under the lower board

# stacking pin columns (0.9" apart, 11 positions)
STK_XL = -13.2
STK_XR = 10.0
STK_N = 11
STK_Y0 = 12.7

# extra 4-way stacking strip near the front
STK4_Y = -15.57
STK4_X0 = -5.55


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cbox(cx, cy, sx, sy, z0, h):
    return box(cx - sx / 2, cx + sx / 2, cy - sy / 2, cy + sy / 2, z0, z0 + h)


def square_pin(z0, z1, tip_top=0.5, tip_bot=0.5, top_frac=0.35, bot_frac=0.35):
    """square pin along Z from z0 to z1 with tapered (pyramidal) ends."""
    w = PIN_W
    body = (cq.Workplane("XY").workplane(offset=z0 + tip_bot)
            .rect(w, w).extrude((z1 - tip_top) - (z0 + tip_bot)))
    top = (cq.Workplane("XY").workplane(offset=z1 - tip_top)
           .rect(w, w).workplane(offset=tip_top).rect(w * top_frac, w * top_frac)
           .loft())
    bot = (cq.Workplane("XY").workplane(offset=z0 + tip_bot)
           .rect(w, w).workplane(offset=-tip_bot).rect(w * bot_frac, w * bot_frac)
           .loft())
    return body.union(top).union(bot).val()


def vault_pin(z0, z1, tip_top=0.75, tip_bot=0.55):
    """square pin whose ends are rounded into a cloister-vault (bullet) tip."""
    w = PIN_W
    body = (cq.Workplane("XY").workplane(offset=z0 + tip_bot)
            .rect(w, w).extrude((z1 - tip_top) - (z0 + tip_bot)))

    def tip(L):
        # pointed (gothic) arch in both vertical planes -> cloister-vault tip
        c = (L * L - w * w / 4.0) / w
        r = c + w / 2.0
        t = cq.Workplane("XY").box(w, w, L, centered=(True, True, False))
        for sgn in (-1, 1):
            cy = cq.Workplane("XZ").center(sgn * c, 0).circle(r).extrude(w, both=True)
            cx = cq.Workplane("YZ").center(sgn * c, 0).circle(r).extrude(w, both=True)
            t = t.intersect(cy).intersect(cx)
        return t

    top = tip(tip_top).translate((0, 0, z1 - tip_top))
    bot = tip(tip_bot).mirror("XY").translate((0, 0, z0 + tip_bot))
    return body.union(top).union(bot).val()


def at(shape, x, y, z=0.0):
    return shape.moved(cq.Location(cq.Vector(x, y, z)))


parts = []       # list of cq.Shape to fuse with the top board
cuts = []        # shapes to subtract from the top board

# ---------------------------------------------------------------------------
# boards
# ---------------------------------------------------------------------------
top_board = box(-TB_W / 2, TB_W / 2, -TB_L / 2, TB_L / 2, -TB_T, 0.0)
lower_board = box(LB_X0, LB_X1, LB_Y0, LB_Y1, LB_BOT, LB_TOP)
parts.append(lower_board.val())

# ---------------------------------------------------------------------------
# pin headers on the top board
# ---------------------------------------------------------------------------
hdr_pin = square_pin(-TB_T - HDR_PIN_BELOW, HDR_PIN_TOP,
                     tip_top=0.22, tip_bot=0.22, top_frac=0.45, bot_frac=0.45)

GROOVE = 0.24       # V-notch between header positions
CORNER = 0.28       # chamfer on the outer vertical corners


def header_base(n):
    """moulded plastic body of an n-way 2.54 mm header, first pin at x=0"""
    body = (cq.Workplane("XY").box(n * PITCH, PITCH, HDR_BASE_H, centered=(False, True, False))
            .translate((-PITCH / 2, 0, 0))
            .edges("|Z").chamfer(CORNER))
    for i in range(1, n):
        xj = -PITCH / 2 + i * PITCH
        for sgn in (-1, 1):
            yo = sgn * (PITCH / 2 + 0.05)
            yi = sgn * (PITCH / 2 - GROOVE)
            d = GROOVE + 0.05
            tri = (cq.Workplane("XY").workplane(offset=-0.01)
                   .polyline([(xj - d, yo), (xj + d, yo), (xj, yi)]).close()
                   .extrude(HDR_BASE_H + 0.02))
            body = body.cut(tri)
    return body.val()


HEADERS = [
    # (first pin X, Y, count)   all rows run along X
    (-11.43, 17.70, 2),
    (7.50, 16.70, 2),
    (-8.14, 1.83, 3),
    (-1.64, -2.16, 4),
    (-1.64, -4.96, 4),
    (-9.94, -7.16, 3),
    (-9.94, -10.36, 3),
    (-1.64, -10.36, 4),
    (-1.64, -16.14, 4),
    (-13.00, -21.25, 1),
    (-9.20, -21.25, 3),
    (0.25, -21.25, 4),
    (12.55, 4.18, 1),
]

base_cache = {}
for (x0, y, n) in HEADERS:
    if n not in base_cache:
        base_cache[n] = header_base(n)
    parts.append(at(base_cache[n], x0, y, 0.0))
    for i in range(n):
        parts.append(at(hdr_pin, x0 + i * PITCH, y))

# ---------------------------------------------------------------------------
# stacking pins (through both boards) and female sockets between the boards
# ---------------------------------------------------------------------------
stk_pin = vault_pin(LB_BOT - STK_PIN_BELOW, STK_PIN_TOP, tip_top=0.75, tip_bot=0.55)

sock_unit = (cq.Workplane("XY").box(PITCH, PITCH, GAP, centered=(True, True, False))
             .edges("|Z").chamfer(0.22)).val()

RING_D = 1.25
ring = cq.Workplane("XY").circle(RING_D / 2).extrude(0.4).translate((0, 0, -0.4)).val()

NO_RING = {(STK_XL, 3), (STK_XL, 4)}
for xc in (STK_XL, STK_XR):
    for k in range(STK_N):
        y = STK_Y0 - k * PITCH
        parts.append(at(stk_pin, xc, y))
        parts.append(at(sock_unit, xc, y, LB_TOP))
        if (xc, k) not in NO_RING:
            cuts.append(at(ring, xc, y))

sock4 = (cq.Workplane("XY").box(2.3, 2.3, GAP, centered=(True, True, False))
         .edges("|Z").chamfer(0.2)).val()
for i in range(4):
    x = STK4_X0 + i * PITCH
    parts.append(at(stk_pin, x, STK4_Y))
    parts.append(at(sock4, x, STK4_Y, LB_TOP))

# ---------------------------------------------------------------------------
# mini-USB receptacle at the back edge (opening faces +Y)
# ---------------------------------------------------------------------------
USB_X0, USB_X1 = -4.92, 2.68
USB_Y0, USB_Y1 = 15.8, 25.05
USB_H = 4.0
usb_cx = (USB_X0 + USB_X1) / 2
usb_w = USB_X1 - USB_X0

usb = box(USB_X0, USB_X1, USB_Y0, USB_Y1, 0.0, USB_H)
usb = usb.faces("<Y").edges(">Z").fillet(1.0)
usb = usb.edges("|Y and >Z").fillet(0.55)
# the shell stops short of the board at the front: the contact leads exit there
usb = usb.cut(box(USB_X0 + 0.9, USB_X1 - 0.9, USB_Y0 - 0.1, USB_Y0 + 1.2, -0.1, 1.1))
for i in range(5):
    lx = usb_cx - 1.6 + i * 0.8
    usb = usb.union(box(lx - 0.15, lx + 0.15, USB_Y0 - 0.5, USB_Y0 + 1.3, 0.0, 0.15))
# pill shaped recess pressed into the front face
pill = (cq.Workplane("XZ", origin=(0, USB_Y0 - 0.05, 0))
        .center(usb_cx - 0.5, 2.45).slot2D(4.4, 0.55).extrude(-0.25))
usb = usb.cut(pill)
# trapezoidal mouth at the back
mouth = (cq.Workplane("XZ", origin=(0, USB_Y1 + 0.01, 0))
         .polyline([(usb_cx - 2.7, 2.8), (usb_cx + 2.7, 2.8),
                    (usb_cx + 2.7, 1.6), (usb_cx + 2.0, 0.85),
                    (usb_cx - 2.0, 0.85), (usb_cx - 2.7, 1.6)]).close()
         .extrude(5.5))
usb = usb.cut(mouth)
# inner tongue with five contacts
usb = usb.union(box(usb_cx - 2.1, usb_cx + 2.1, USB_Y1 - 5.6, USB_Y1 - 0.7, 1.95, 2.45))
for i in range(5):
    lx = usb_cx - 1.6 + i * 0.8
    usb = usb.union(box(lx - 0.13, lx + 0.13, USB_Y1 - 5.0, USB_Y1 - 0.9, 1.75, 1.95))
# two U-shaped spring slots and a latch window stamped in the top of the shell
for (ux0, ux1) in ((-4.23, -2.05), (0.23, 2.03)):
    u_cut = box(ux0, ux1, 20.2, 23.95, USB_H - 0.3, USB_H + 0.3)
    u_cut = u_cut.edges("|Z and >Y").fillet(0.3)
    u_cut = u_cut.cut(box(ux0 + 0.4, ux1 - 0.4, 20.1, 23.5, USB_H - 0.4, USB_H + 0.4))
    usb = usb.cut(u_cut)
usb = usb.cut(cbox(-0.35, 22.0, 0.4, 4.0, USB_H - 0.3, 0.6))
usb = usb.cut(cbox(-0.9, 18.6, 1.0, 1.4, USB_H - 0.3, 0.6))
usb = usb.cut(cbox(usb_cx - 2.4, 17.6, 1.9, 0.4, USB_H - 0.3, 0.6))
# horizontal stiffening groove on both side walls
for sx in (USB_X0, USB_X1):
    usb = usb.cut(cbox(sx, 20.8, 0.3, 5.0, 1.55, 0.3))
# J-shaped mounting legs on both sides (front and rear)
for ty in (16.6, 22.4):
    for sx, sgn in ((USB_X0, -1), (USB_X1, 1)):
        leg = box(min(sx, sx + sgn * 0.35), max(sx, sx + sgn * 0.35), ty - 0.6, ty + 0.6, 0.0, 2.6)
        foot = box(min(sx, sx + sgn * 0.9), max(sx, sx + sgn * 0.9), ty - 0.6, ty + 0.6, 0.0, 0.3)
        usb = usb.union(leg).union(foot)
parts.append(usb.val())

# ---------------------------------------------------------------------------
# SMD parts on the top board
# ---------------------------------------------------------------------------
def chip(cx, cy, sx, sy, h, cap=0.35):
    """two-terminal SMD part: body plus slightly proud end caps along its long axis"""
    b = cbox(cx, cy, sx, sy, 0.0, h)
    if sx >= sy:
        c1 = cbox(cx - sx / 2 + cap / 2, cy, cap, sy + 0.06, 0.0, h + 0.06)
        c2 = cbox(cx + sx / 2 - cap / 2, cy, cap, sy + 0.06, 0.0, h + 0.06)
    else:
        c1 = cbox(cx, cy - sy / 2 + cap / 2, sx + 0.06, cap, 0.0, h + 0.06)
        c2 = cbox(cx, cy + sy / 2 - cap / 2, sx + 0.06, cap, 0.0, h + 0.06)
    return b.union(c1).union(c2).val()


# resistors / capacitors (0805 / 1206)
R_SMALL = [
    (-6.24, 8.01, True),
    (-10.08, 6.40, False),
    (-2.41, 7.30, False),
    (0.15, 7.30, False),
    (5.86, 0.42, True),
    (-9.28, -4.70, True),
    (12.82, 8.42, False),
    (12.55, 0.34, False),
    (7.37, 20.20, True),
]
for (x, y, horiz) in R_SMALL:
    if horiz:
        parts.append(chip(x, y, 1.8, 1.2, 0.45))
    else:
        parts.append(chip(x, y, 1.2, 1.8, 0.45))
parts.append(chip(-5.85, -2.16, 3.0, 1.6, 0.55, cap=0.5))

# two larger moulded parts (crystal / capacitor style with wrap-around end caps)
for (x0, x1, y0, y1, h) in [(-12.8, -9.9, 20.7, 23.2, 2.4), (1.0, 3.94, 11.4, 13.85, 2.65)]:
    body = box(x0 + 0.18, x1 - 0.18, y0 + 0.08, y1 - 0.08, 0.0, h)
    body = body.union(box(x0, x0 + 0.18, y0, y1, 0.0, h - 0.05))
    body = body.union(box(x1 - 0.18, x1, y0, y1, 0.0, h - 0.05))
    parts.append(body.val())

# SMD diode / LED with a round lens at one end
d1 = cbox(-10.58, 13.85, 1.9, 2.7, 0.0, 1.05).edges("|Y and >Z").chamfer(0.2)
d1 = d1.cut(cbox(-10.58, 14.2, 2.2, 0.45, 0.78, 0.5))
lens = (cq.Workplane("XY").circle(0.6).circle(0.35).extrude(0.9)
        .translate((-10.75, 12.05, 0.0)))
d1 = d1.union(lens)
parts.append(d1.val())

# SOT-89 regulator (drafted moulded body)
u1 = (cq.Workplane("XY").rect(2.7, 4.4).extrude(1.6, taper=6)
      .translate((-6.03, 12.38, 0.0)))
u1 = u1.faces(">Z").edges().chamfer(0.15)
u1 = u1.cut(cq.Workplane("XY").circle(0.3).extrude(0.1).translate((-6.0, 12.4, 1.52)))
for ly in (13.85, 12.37, 10.9):
    u1 = u1.union(cbox(-7.75, ly, 1.0, 0.5, 0.0, 0.25))
u1 = u1.union(cbox(-4.45, 11.9, 0.7, 1.5, 0.0, 0.3))
parts.append(u1.val())

# SOT-23 transistor
q1 = cbox(-5.64, 5.08, 3.0, 1.4, 0.0, 1.0).edges(">Z").chamfer(0.12)
for (lx, ly) in [(-6.6, 6.1), (-4.7, 6.1), (-5.64, 4.05)]:
    q1 = q1.union(cbox(lx, ly, 0.45, 0.7, 0.0, 0.25))
parts.append(q1.val())

# ---------------------------------------------------------------------------
# parts on the underside of the lower board
# ---------------------------------------------------------------------------
def under(x0, x1, y0, y1, h):
    return box(x0, x1, y0, y1, LB_BOT - h, LB_BOT)

# large QFN controller
qfn = under(-0.67, 5.38, -9.63, -3.46, 0.9).faces("<Z").edges().chamfer(0.3)
parts.append(qfn.val())
# smaller, thicker package (crystal-oscillator style, rounded corners)
u3 = (under(-9.4, -4.1, -9.3, -5.1, 1.6).edges("|Z").fillet(0.45)
      .faces("<Z").edges().chamfer(0.2))
parts.append(u3.val())
# small two-tier connector / switch at the front-left corner
conn = under(-10.74, -7.64, -16.3, -13.9, 2.24).faces("<Z").edges().chamfer(0.2)
conn = conn.union(under(-7.64, -5.79, -16.1, -14.1, 2.0))
parts.append(conn.val())
# SOT-23-5 style part with leads
sot = under(-4.55, -1.65, 0.6, 3.0, 1.1).faces("<Z").edges().chamfer(0.12)
for lx in (-4.05, -3.1, -2.15):
    sot = sot.union(under(lx - 0.2, lx + 0.2, 0.1, 0.7, 0.3))
    sot = sot.union(under(lx - 0.2, lx + 0.2, 2.9, 3.5, 0.3))
parts.append(sot.val())
# passives (0603)
PASSIVES_UNDER = [
    (0.95, -11.57, True),
    (-9.39, 1.15, False), (-7.76, 1.28, False), (-6.27, 1.30, False),
    (-9.42, 3.78, True), (-8.10, 5.10, True),
    (0.63, 1.97, True), (2.44, 1.92, True),
    (5.60, 3.66, True), (5.25, 6.94, True),
]
for (x, y, horiz) in PASSIVES_UNDER:
    sx, sy = (1.6, 0.8) if horiz else (0.8, 1.6)
    parts.append(cbox(x, y, sx, sy, LB_BOT - 0.5, 0.5).val())

# ---------------------------------------------------------------------------
# assemble
# ---------------------------------------------------------------------------
tb = top_board.val()
for c in cuts:
    tb = tb.cut(c)

solid = tb.fuse(*parts).clean()
result = cq.Workplane("XY").newObject([solid])
